import cadquery as cq

# ---------------- overall layout ----------------
W = 60.0          # outer width (X) of each half
L = 107.0         # outer length (Y) of each half
GAP = 10.7        # gap between the two halves (X)
T = 2.1           # wall thickness
FLOOR = 1.2       # floor thickness

# ---------------- shallow half (lid / tray, at -X) ----------------
H1 = 17.0                 # height of tray
RAB_W = 1.05              # inner rabbet width on the rim
RAB_D = 1.6               # inner rabbet depth
LEDGE1_H = 2.2            # ledge height above floor
LEDGE1_GAP = 1.3          # gap between ledge ends and side walls
LEDGE1_PY = (L / 2 - 13.1, L / 2 - 5.7)     # +Y ledge y-range
LEDGE1_NY = (-L / 2 + 13.0, -L / 2 + 20.1)  # -Y ledge y-range
POST1_D = 4.2             # tray PCB posts
POST1_H = 6.1
POST1_X = 17.7
POST1_CX = -0.22
POST1_Y = (L / 2 - 9.4, -L / 2 + 16.7)
SLOT_L = 19.7             # wall vent slot length (Y)
SLOT_H = 3.16             # wall vent slot height (Z)
SLOT_PITCH_Y = 22.5
SLOT_Z = (6.35, 11.95)
SLOT_CY = 3.0             # y-centre of the slot group
TEXT = "Bottom Text"
TEXT_SIZE = 14.2
TEXT_SQUEEZE = 0.855      # width factor of the lettering
TEXT_CX = -1.9            # text centre offset (X) on the underside
TEXT_CY = 3.4             # text centre offset (Y)
TEXT_DEPTH = 0.5
BOT_HOLE_D = 3.4          # underside recesses under the posts
BOT_HOLE_DEPTH = 0.5

# ---------------- deep half (base box, at +X) ----------------
H2 = 31.3                 # wall height
LIP_H = 1.6               # raised inner lip height
LIP_W = 1.05              # raised inner lip width
WIN_W = 14.55             # window in -Y wall
WIN_CX = 0.45
WIN_Z0, WIN_Z1 = 16.7, 25.65
BLOCK_W = 26.2            # standoff block size
BLOCK_D = 5.9
BLOCK_CX = 1.1            # blocks sit slightly off-centre in X
BLOCK_TOP = 16.6
BLOCK_PY = L / 2 - 15.9   # +Y block centre
BLOCK_NY = -L / 2 + 8.45  # -Y block centre
POST2_D = 3.4             # box PCB posts
POST2_H = 7.35
POST2_CX = 0.33
POST2_X = 10.05
POST2_Y = (L / 2 - 15.95, -L / 2 + 8.5)
VENT_W = 3.7              # floor vent slots
VENT_CY = -3.3
VENTS = [(3.03, 52.1), (9.08, 43.3), (15.13, 43.3)]  # (x offset, length)
OUTER_VENT = (21.5, 31.2)
VENT_CX = -0.4
VHOLE_D = 6.0             # round floor holes
VHOLE_X = 21.35
OUTER_CX = -0.1           # centre of the outer slot pair / round holes
VHOLE_DY = 21.4

XC = W / 2 + GAP / 2


def open_box(h):
    outer = cq.Workplane("XY").box(W, L, h, centered=(True, True, False))
    inner = (cq.Workplane("XY").workplane(offset=FLOOR)
             .rect(W - 2 * T, L - 2 * T).extrude(h))
    return outer.cut(inner)


# ======== shallow tray ========
tray = open_box(H1)
# rabbet around the inside of the rim
rab = (cq.Workplane("XY").workplane(offset=H1 - RAB_D)
       .rect(W - 2 * T + 2 * RAB_W, L - 2 * T + 2 * RAB_W).extrude(RAB_D + 1))
tray = tray.cut(rab)

# ledges with posts
lx = W - 2 * T - 2 * LEDGE1_GAP
for (y0, y1) in (LEDGE1_PY, LEDGE1_NY):
    ledge = (cq.Workplane("XY").workplane(offset=FLOOR)
             .center(0, (y0 + y1) / 2).rect(lx, y1 - y0).extrude(LEDGE1_H))
    tray = tray.union(ledge)
for py in POST1_Y:
    posts = (cq.Workplane("XY").workplane(offset=FLOOR + LEDGE1_H)
             .pushPoints([(POST1_CX - POST1_X, py), (POST1_CX + POST1_X, py)])
             .circle(POST1_D / 2).extrude(POST1_H))
    tray = tray.union(posts)

# vent slots through both long walls (2 rows x 3)
slot_pts = []
for i in (-1, 0, 1):
    for z in SLOT_Z:
        slot_pts.append((SLOT_CY + i * SLOT_PITCH_Y, z))
slots = (cq.Workplane("YZ").workplane(offset=-W)
         .pushPoints(slot_pts).rect(SLOT_L, SLOT_H).extrude(2 * W))
tray = tray.cut(slots)

# shallow round recesses in the underside below the posts
bh = (cq.Workplane("XY")
      .pushPoints([(POST1_CX + sx * POST1_X, py) for sx in (-1, 1) for py in POST1_Y])
      .circle(BOT_HOLE_D / 2).extrude(BOT_HOLE_DEPTH))
tray = tray.cut(bh)

# engraved text on the underside (reads correctly seen from below)
try:
    txt_wp = cq.Workplane(cq.Plane(origin=(0, 0, 0), xDir=(0, 1, 0), normal=(0, 0, -1)))
    txt = txt_wp.text(TEXT, TEXT_SIZE, -TEXT_DEPTH, kind="bold",
                      halign="center", valign="center").val()
    try:
        # condense the lettering along the reading direction (world Y)
        from OCP.gp import gp_GTrsf
        from OCP.BRepBuilderAPI import BRepBuilderAPI_GTransform
        gt = gp_GTrsf()
        gt.SetValue(2, 2, TEXT_SQUEEZE)
        txt = cq.Shape.cast(BRepBuilderAPI_GTransform(txt.wrapped, gt, True).Shape())
    except Exception:
        pass
    txt = txt.translate(cq.Vector(TEXT_CX, TEXT_CY, 0))
    tray = tray.cut(cq.Workplane("XY").add(txt))
except Exception:
    pass

tray = tray.translate((-XC, 0, 0))

# ======== deep box ========
box = open_box(H2)
lip = (cq.Workplane("XY").workplane(offset=H2)
       .rect(W - 2 * T + 2 * LIP_W, L - 2 * T + 2 * LIP_W)
       .rect(W - 2 * T, L - 2 * T).extrude(LIP_H))
box = box.union(lip)

# window in the -Y wall
win = (cq.Workplane("XZ").workplane(offset=L / 2 - T - 1)
       .center(WIN_CX, (WIN_Z0 + WIN_Z1) / 2).rect(WIN_W, WIN_Z1 - WIN_Z0).extrude(T + 2))
box = box.cut(win)

# standoff blocks with posts
for by in (BLOCK_PY, BLOCK_NY):
    blk = (cq.Workplane("XY").workplane(offset=FLOOR / 2)
           .center(BLOCK_CX, by).rect(BLOCK_W, BLOCK_D).extrude(BLOCK_TOP - FLOOR / 2))
    box = box.union(blk)
for py in POST2_Y:
    posts = (cq.Workplane("XY").workplane(offset=BLOCK_TOP)
             .pushPoints([(POST2_CX - POST2_X, py), (POST2_CX + POST2_X, py)])
             .circle(POST2_D / 2).extrude(POST2_H))
    box = box.union(posts)

# floor vent slots and round holes
vpts = []
for (vx, vl) in VENTS:
    for sx in (-1, 1):
        vpts.append((VENT_CX + sx * vx, vl))
for sx in (-1, 1):
    vpts.append((OUTER_CX + sx * OUTER_VENT[0], OUTER_VENT[1]))
for (vx, vl) in vpts:
    v = (cq.Workplane("XY").workplane(offset=-1)
         .center(vx, VENT_CY).rect(VENT_W, vl).extrude(FLOOR + 2))
    box = box.cut(v)
vh = (cq.Workplane("XY").workplane(offset=-1)
      .pushPoints([(OUTER_CX + sx * VHOLE_X, VENT_CY + sy * VHOLE_DY) for sx in (-1, 1) for sy in (-1, 1)])
      .circle(VHOLE_D / 2).extrude(FLOOR + 2))
box = box.cut(vh)

# shallow round recesses in the underside below the standoff posts
bh2 = (cq.Workplane("XY")
       .pushPoints([(POST2_CX + sx * POST2_X, py) for sx in (-1, 1) for py in POST2_Y])
       .circle(BOT_HOLE_D / 2).extrude(BOT_HOLE_DEPTH))
box = box.cut(bh2)

box = box.translate((XC, 0, 0))

result = tray.union(box)

VIEW = {"azimuth": 45, "elevation": 26}
